import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 50.0            # dome outer radius (= base ring outer radius, flush)
SHELL_T = 0.7       # dome skin thickness
HF = 4.13           # base ring height (dome equator sits on top of it)
RING_T = 1.8        # radial wall thickness of the base ring
SLOT_W = 22.75      # width of the observation slot (along Y), slot runs along X

NOTCH_W = 3.5       # notch width in the base ring
NOTCH_H = 3.4       # notch height (from the bottom of the ring)
NOTCH_ANGLES = [45, 135, 225, 315]

# internal stiffening fins: thin plates perpendicular to X filling each half,
# visible through the open slot faces and the open underside
FIN_PITCH = 2.9     # spacing of the fins along X (one fin on the centre line)
FIN_T = 0.75        # fin thickness
BAR_W = 1.5         # bottom bar along each slot edge: width (Y)
BAR_H = 1.4         # bottom bar height (Z)

VIEW = {"azimuth": 45, "elevation": 26}

RI = R - RING_T
RIN = R - SHELL_T
big = 4 * R

half_space = cq.Workplane("XY").box(big, big, R + 1, centered=(True, True, False))

# ---------------- dome skin ----------------
outer = cq.Workplane("XY").sphere(R).intersect(half_space)
inner = cq.Workplane("XY").sphere(RIN).intersect(half_space)
shell = outer.cut(inner)

# ---------------- fins ----------------
# only fins that reach past the slot plane (the slot removes the rest)
x_lim = math.sqrt(RIN ** 2 - (SLOT_W / 2) ** 2) - FIN_T / 2 - 0.05
n = int(x_lim / FIN_PITCH)
xs = [k * FIN_PITCH for k in range(-n, n + 1)]
fins = (
    cq.Workplane("XY")
    .pushPoints([(x, 0) for x in xs])
    .rect(FIN_T, 2 * R)
    .extrude(R)
    .intersect(inner)
)

# ---------------- bottom bars along the slot edges ----------------
bars = None
for side in (1, -1):
    b = (
        cq.Workplane("XY")
        .box(2 * R, BAR_W, BAR_H, centered=(True, True, False))
        .translate((0, side * (SLOT_W / 2 + BAR_W / 2), 0))
    )
    bars = b if bars is None else bars.union(b)
bars = bars.intersect(inner)

body = shell.union(fins).union(bars)

# ---------------- observation slot ----------------
slot = cq.Workplane("XY").box(big, SLOT_W, big, centered=(True, True, False)).translate((0, 0, -0.01))
body = body.cut(slot).translate((0, 0, HF))

# ---------------- base ring with notches ----------------
ring = cq.Workplane("XY").circle(R).circle(RI).extrude(HF)
for a in NOTCH_ANGLES:
    cutter = (
        cq.Workplane("XY")
        .box(RING_T + 4, NOTCH_W, NOTCH_H * 2, centered=(True, True, True))
        .translate((R - RING_T / 2, 0, 0))
        .rotate((0, 0, 0), (0, 0, 1), a)
    )
    ring = ring.cut(cutter)

result = body.union(ring)
